import math
import cadquery as cq

# ============ driving dimensions (mm) ============
# Cord spool: axis along Y, thin flange at the front (-Y), thick flange at the back (+Y)
D_FLANGE = 50.0        # outer diameter of both flanges
D_BORE = 10.0          # central through bore
T_FRONT = 5.75         # front (-Y) flange thickness
L_DRUM = 38.35         # length of the grooved drum between the flanges
T_BACK = 14.35         # back (+Y) flange thickness
D_CREST = 40.0         # drum crest diameter

# helical cord groove (left-hand, round bottom, sharp crests)
PITCH = 3.36
GROOVE_DEPTH = 1.06
CREST_LAND = 0.10      # tiny land left on the crest
GROOVE_PHASE = 5.53    # groove centre at the top (+Z) measured from the front face

# back face: nut trap slot + radial set-screw hole on the -X side
NUT_W = 4.7            # slot width (X)
NUT_H = 12.0           # slot height (Z)
NUT_DEPTH = 11.0       # slot depth into the back face
NUT_X = -8.45          # slot centre X
SET_D = 5.8            # radial set-screw hole diameter
SET_FROM_BACK = 5.15   # set-screw axis distance from the back face

# slanted cord entry hole through the front flange
CORD_D = 4.4
CORD_ENTRY = (-14.0, -14.5)   # (x, z) of the hole centre on the front face
CORD_TILT = 62.0              # tilt of the hole axis from the spool axis (deg)
CORD_DIR = -31.8              # direction of the tilt in the XZ plane (deg from +X)

VIEW = {"azimuth": 45, "elevation": 26}

# ============ derived ============
L_TOTAL = T_FRONT + L_DRUM + T_BACK
Y0 = -L_TOTAL / 2.0                # front face
Y1 = L_TOTAL / 2.0                 # back face
YS = Y0 + T_FRONT                  # drum start
YE = YS + L_DRUM                   # drum end
R_F = D_FLANGE / 2.0
R_B = D_BORE / 2.0
R_C = D_CREST / 2.0

half_w = PITCH / 2.0 - CREST_LAND / 2.0
R_G = (half_w ** 2 + GROOVE_DEPTH ** 2) / (2.0 * GROOVE_DEPTH)   # groove radius
R_GC = R_C + math.sqrt(R_G ** 2 - half_w ** 2)                   # groove centre radius
R_ROOT = R_GC - R_G


SEAM_ROT = 215.0   # turn the cylinder seams towards the lower back-left, out of the main views


def cyl(r, y_from, y_to):
    c = cq.Solid.makeCylinder(r, y_to - y_from, cq.Vector(0, y_from, 0), cq.Vector(0, 1, 0))
    return c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), SEAM_ROT)


# ---------- helical groove cut into the drum ----------
def helical_drum():
    drum = cyl(R_C, YS, YE)
    r_cut = R_C + 0.03
    wc = math.sqrt(R_G ** 2 - (R_GC - r_cut) ** 2)
    # each turn is swept from the top (+Z) and then turned by SEAM_ROT about the axis, so the
    # start height is shifted to keep the groove at Y0 + GROOVE_PHASE on the top
    y0 = Y0 + GROOVE_PHASE - PITCH * (SEAM_ROT % 360.0) / 360.0
    while y0 + wc > YS - 0.2:
        y0 -= PITCH
    n_turns = int(math.ceil((YE + wc + 0.2 - y0) / PITCH))
    tubes = []
    for k in range(n_turns):
        yk = y0 + k * PITCH
        helix = cq.Wire.makeHelix(PITCH, PITCH, R_GC, center=cq.Vector(0, yk, 0),
                                  dir=cq.Vector(0, 1, 0), lefthand=True)
        prof = (
            cq.Workplane("YZ")
            .moveTo(yk - wc, r_cut)
            .threePointArc((yk, R_ROOT), (yk + wc, r_cut))
            .close()
        )
        tube = prof.sweep(cq.Workplane("XY").add(helix), isFrenet=True).val()
        tubes.append(tube.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), SEAM_ROT))
    before = drum.Volume()
    drum = drum.cut(*tubes)          # one boolean, one tool per turn
    removed = before - drum.Volume()
    return drum, removed


def annular_drum():
    # fallback: same groove profile as plain rings
    prof = cq.Workplane("XY").moveTo(R_B, YS).lineTo(R_C, YS)
    n = int(L_DRUM // PITCH)
    a0 = YS + (L_DRUM - n * PITCH) / 2.0
    prof = prof.lineTo(R_C, a0)
    for i in range(n):
        a = a0 + i * PITCH
        prof = prof.threePointArc((R_ROOT, a + PITCH / 2.0), (R_C, a + PITCH))
    prof = prof.lineTo(R_C, YE).lineTo(R_B, YE).close()
    return prof.revolve(360.0, (0, 0, 0), (0, 1, 0)).val()


drum = None
try:
    drum, removed = helical_drum()
    # sanity check of the helical cut (about one groove section per pitch of drum)
    seg_area = R_G ** 2 * math.acos((R_GC - R_C) / R_G) - (R_GC - R_C) * half_w
    expect = seg_area * 2.0 * math.pi * (R_GC - R_G / 2.0) * L_DRUM / PITCH
    if (not drum.isValid()) or abs(removed - expect) > 0.25 * expect:
        drum = None
except Exception:
    drum = None
if drum is None:
    drum = annular_drum()

# ---------- flanges + drum ----------
front = cyl(R_F, Y0, YS)
back = cyl(R_F, YE, Y1)
body = cq.Workplane("XY").add(front).union(cq.Workplane("XY").add(drum)).union(
    cq.Workplane("XY").add(back))

# central bore
body = body.cut(cq.Workplane("XY").add(cyl(R_B, Y0 - 1.0, Y1 + 1.0)))

# ---------- nut trap slot in the back face ----------
pocket = (
    cq.Workplane("XZ", origin=(0, Y1, 0))
    .center(NUT_X, 0)
    .rect(NUT_W, NUT_H)
    .extrude(NUT_DEPTH)            # XZ normal is -Y: into the part
)
body = body.cut(pocket)

# ---------- radial set-screw hole (-X side, into the bore) ----------
y_set = Y1 - SET_FROM_BACK
set_hole = cq.Solid.makeCylinder(SET_D / 2.0, R_F - R_B + 2.0,
                                 cq.Vector(-R_F - 1.0, y_set, 0), cq.Vector(1, 0, 0))
body = body.cut(cq.Workplane("XY").add(set_hole))

# ---------- slanted cord hole through the front flange ----------
t = math.radians(CORD_TILT)
d = math.radians(CORD_DIR)
axis = cq.Vector(math.sin(t) * math.cos(d), math.cos(t), math.sin(t) * math.sin(d))
p0 = cq.Vector(CORD_ENTRY[0], Y0, CORD_ENTRY[1])
run = T_FRONT / math.cos(t)
back_off = (CORD_D / 2.0 * math.sin(t) + 1.0) / math.cos(t)   # keep the end caps clear of the faces
start = p0 - axis * back_off
u_dir = cq.Vector(math.cos(d), 0, math.sin(d))
seam_dir = (u_dir - axis * u_dir.dot(axis)).normalized()    # seam on the hidden far wall
cord = (
    cq.Workplane(cq.Plane(origin=start, xDir=seam_dir, normal=axis))
    .circle(CORD_D / 2.0)
    .extrude(run + 2.0 * back_off)
)
body = body.cut(cord)

result = body
